import cadquery as cq

# ---------------------------------------------------------------------------
# 16 x 16 square-cell grid (LED-matrix style diffuser grid)
# Plate lies in the XZ plane, thickness along Y (front face at -Y, back at +Y).
# The vertical (constant-X) inner walls carry a shallow rectangular clearance
# notch on the back edge, centred in every wall span between the horizontal walls.
# ---------------------------------------------------------------------------

N_X = 16            # cells across (X)
N_Z = 16            # cells up (Z)
PITCH = 10.0        # cell pitch
WALL = 1.0          # inner wall thickness
OUTER = 0.5         # outer frame wall thickness (half an inner wall)
DEPTH = 10.0        # grid depth (Y)

NOTCH_W = 5.5       # clearance notch width along Z (per wall span)
NOTCH_D = 1.5       # clearance notch depth from the back face

CELL = PITCH - WALL
W = N_X * CELL + (N_X - 1) * WALL + 2 * OUTER      # overall width  (X)
H = N_Z * CELL + (N_Z - 1) * WALL + 2 * OUTER      # overall height (Z)

# --- solid plate ------------------------------------------------------------
plate = cq.Workplane("XZ").rect(W, H).extrude(DEPTH / 2.0, both=True)

# --- through cells (rectangular pattern) ------------------------------------
cell_pts = [((i - (N_X - 1) / 2.0) * PITCH, (j - (N_Z - 1) / 2.0) * PITCH)
            for i in range(N_X) for j in range(N_Z)]
cells = (cq.Workplane("XZ").pushPoints(cell_pts).rect(CELL, CELL)
         .extrude(DEPTH, both=True))
grid = plate.cut(cells)

# --- back-edge notches in the vertical walls ---------------------------------
# one long slot per row of cells: spans from the centre of the first cell to
# the centre of the last cell in X (so only the inner vertical walls are hit,
# never the outer frame), NOTCH_W tall in Z, NOTCH_D deep from the back face.
slot_len = (N_X - 1) * PITCH
row_pts = [(0.0, (j - (N_Z - 1) / 2.0) * PITCH) for j in range(N_Z)]
over = 0.5
notches = (cq.Workplane("XZ").workplane(offset=-(DEPTH / 2.0 + over))
           .pushPoints(row_pts).rect(slot_len, NOTCH_W)
           .extrude(NOTCH_D + over))

result = grid.cut(notches)

VIEW = {"azimuth": 45, "elevation": 26}
